import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
PLATE_W = 40.0          # width of each stadium plate (X)
PLATE_H = 100.0         # height of each stadium plate (Z)
T_FRONT = 12.25         # front plate thickness (Y-)
T_BACK = 14.6           # back plate thickness (Y+)
GAP = 41.45             # clear gap between the plates (Y)

SPIGOT_D = 36.2         # bottom spigot diameter
SPIGOT_H = 7.4          # spigot height
FLANGE_D = 37.8         # flange diameter
FLANGE_H = 3.66         # flange thickness
RECESS_D = 32.8         # recess in the spigot bottom
RECESS_DEPTH = 9.0

PLATE_Z0 = 8.6          # bottom of plates above spigot bottom

BAR_R = 12.15           # half width of connector / radius of its round top
BAR_Z = 27.8            # centre height of the round top
BAR_RC = 7.1            # lower corner radius of the connector section
FIL_X = 1.5             # concave blend stub side (X) -> flange top
FIL_JOINT = 1.0         # fillet where the connector meets the plates

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived ----------------
yi_front = -GAP / 2.0
yi_back = GAP / 2.0
z0 = SPIGOT_H + FLANGE_H                      # flange top = connector bottom
R_FL = FLANGE_D / 2.0
C45 = math.cos(math.radians(45))


def plate(y0, t):
    """Stadium plate in the XZ plane, spanning y0..y0+t."""
    return (
        cq.Workplane("XZ", origin=(0, y0 + t, 0))
        .center(0, PLATE_Z0 + PLATE_H / 2.0)
        .slot2D(PLATE_H, PLATE_W, angle=90)
        .extrude(t)
    )


front = plate(yi_front - T_FRONT, T_FRONT)
back = plate(yi_back, T_BACK)

# base: spigot + flange
spigot = cq.Workplane("XY").circle(SPIGOT_D / 2.0).extrude(SPIGOT_H)
flange = cq.Workplane("XY", origin=(0, 0, SPIGOT_H)).circle(R_FL).extrude(FLANGE_H)

# connector between the plates: round top, flat sides, rounded lower corners,
# sitting on the flange top
a, rc = BAR_R, BAR_RC
conn = (
    cq.Workplane("XZ", origin=(0, yi_back, 0))
    .moveTo(-a + rc, z0)
    .lineTo(a - rc, z0)
    .threePointArc((a - rc + C45 * rc, z0 + rc - C45 * rc), (a, z0 + rc))
    .lineTo(a, BAR_Z)
    .threePointArc((0, BAR_Z + a), (-a, BAR_Z))
    .lineTo(-a, z0 + rc)
    .threePointArc((-a + rc - C45 * rc, z0 + rc - C45 * rc), (-a + rc, z0))
    .close()
    .extrude(GAP)
)

# stub: the flange rim carried up under the connector, trimmed flush with the
# connector sides, with a small concave blend into the flange top
zt = z0 + rc + 2.0
f = FIL_X
side = (
    cq.Workplane("XZ")
    .moveTo(-a - f, z0)
    .lineTo(a + f, z0)
    .threePointArc((a + f - C45 * f, z0 + f - C45 * f), (a, z0 + f))
    .lineTo(a, zt)
    .lineTo(-a, zt)
    .lineTo(-a, z0 + f)
    .threePointArc((-a - f + C45 * f, z0 + f - C45 * f), (-a - f, z0))
    .close()
    .extrude(GAP / 2.0, both=True)
)
rim = cq.Workplane("XY", origin=(0, 0, z0)).circle(R_FL).extrude(zt - z0)
stub = side.intersect(rim)

body = conn.union(stub).union(flange).union(spigot)
result = body.union(front).union(back)


class _JointEdges(cq.Selector):
    """Edges where the connector meets the inner faces of the plates."""

    def filter(self, objs):
        out = []
        for e in objs:
            bb = e.BoundingBox()
            on_face = any(
                abs(bb.ymin - yv) < 1e-3 and abs(bb.ymax - yv) < 1e-3
                for yv in (yi_front, yi_back)
            )
            if on_face and bb.xmax <= BAR_R + 1e-3 and bb.xmin >= -BAR_R - 1e-3 \
                    and bb.zmin >= z0 - 1e-3:
                out.append(e)
        return out


result = result.edges(_JointEdges()).fillet(FIL_JOINT)

# recess in the spigot bottom
result = result.cut(cq.Workplane("XY").circle(RECESS_D / 2.0).extrude(RECESS_DEPTH))
